"""Square spacer / adapter frame.

Front face (-Y) carries a rim with six blind screw holes, four cored slots
between the holes (top and bottom rows) and two long narrow cored slots at
the sides; the slot ends are arcs concentric with the neighbouring holes.
The middle is a deep rectangular pocket whose floor has a large round
through hole.  The back face (+Y) is plain with a big round-over all round.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # outer width  (X)
H = 100.0          # outer height (Z)
T = 28.5           # plate thickness (Y); front face at y = -T/2
R_CORNER = 2.8     # outline corner radius (front view)
R_BACK = 13.0      # big round-over on all back edges

POCKET_W = 75.4    # central rectangular pocket, width  (X)
POCKET_H = 67.5    # central rectangular pocket, height (Z)
POCKET_R = 2.0     # pocket corner radius
POCKET_D = 22.9    # pocket depth from the front face
HOLE_D = 53.8      # big through hole in the pocket floor
HOLE_BACK_R = 1.5  # small round-over of that hole on the back face

BOLT_D = 8.0       # blind screw holes on the rim
BOLT_X = 40.5      # hole position from the centre (X)
BOLT_Z = 40.6      # hole position from the centre (Z)
BOLT_DEPTH = POCKET_D

SLOT_Z_IN = 38.0   # top/bottom slots: inner long edge  |z|
SLOT_Z_OUT = 46.0  # top/bottom slots: outer long edge  |z|
SLOT_END_R = 9.5   # slot ends = arcs of this radius around the hole centres
SLOT_DEPTH = POCKET_D

SIDE_X_IN = 42.0   # side slots: inner long edge |x|
SIDE_X_OUT = 46.0  # side slots: outer long edge |x|
SIDE_DEPTH = POCKET_D

Y_FRONT = -T / 2.0
Y_BACK = T / 2.0


def front_wp():
    """Workplane on the front face: local x = +X, local y = +Z, normal = -Y.
    Negative extrusion distances therefore cut into the part (+Y)."""
    pl = cq.Plane(origin=(0, Y_FRONT, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    return cq.Workplane(pl)


# ---------------- body: rounded square block, back edges rounded ----------------
body = (
    cq.Workplane("XY")
    .box(W, T, H)
    .edges("|Y").fillet(R_CORNER)
    .faces(">Y").edges().fillet(R_BACK)
)

# ---------------- central pocket + big through hole ----------------
pocket = (
    front_wp()
    .rect(POCKET_W, POCKET_H)
    .extrude(-POCKET_D)
    .edges("|Y").fillet(POCKET_R)
)
body = body.cut(pocket)

through = front_wp().circle(HOLE_D / 2.0).extrude(-2.0 * T)
body = body.cut(through)

# small round-over on the back edge of the big hole
body = body.edges(
    cq.selectors.BoxSelector(
        (-HOLE_D / 2 - 1, Y_BACK - 0.5, -HOLE_D / 2 - 1),
        (HOLE_D / 2 + 1, Y_BACK + 0.5, HOLE_D / 2 + 1),
    )
).fillet(HOLE_BACK_R)

# ---------------- six blind screw holes ----------------
bolt_pts = [(sx * BOLT_X, sz * BOLT_Z) for sx in (-1, 1) for sz in (-1, 1)]
bolt_pts += [(0.0, BOLT_Z), (0.0, -BOLT_Z)]
bolts = front_wp().pushPoints(bolt_pts).circle(BOLT_D / 2.0).extrude(-BOLT_DEPTH)
body = body.cut(bolts)


# ---------------- cored slots between the holes ----------------
def arc_slot(s_a, s_b, v_c, v_lo, v_hi, depth, along_x=True):
    """Slot running from hole centre s_a to hole centre s_b (along X if
    along_x, else along Z); both centres lie on the line v = v_c.  The long
    sides are the straight lines v = v_lo and v = v_hi, the ends are concave
    arcs of radius SLOT_END_R concentric with the two holes."""
    R = SLOT_END_R

    def end_a(v):
        return s_a + math.sqrt(R * R - (v - v_c) ** 2)

    def end_b(v):
        return s_b - math.sqrt(R * R - (v - v_c) ** 2)

    def p(s, v):
        return (s, v) if along_x else (v, s)

    v_m = 0.5 * (v_lo + v_hi)
    prof = (
        front_wp()
        .moveTo(*p(end_a(v_lo), v_lo))
        .threePointArc(p(end_a(v_m), v_m), p(end_a(v_hi), v_hi))
        .lineTo(*p(end_b(v_hi), v_hi))
        .threePointArc(p(end_b(v_m), v_m), p(end_b(v_lo), v_lo))
        .close()
    )
    return prof.extrude(-depth)


slots = []
for sz in (-1, 1):                       # top and bottom rows: 2 slots each
    lo, hi = sorted((sz * SLOT_Z_IN, sz * SLOT_Z_OUT))
    for xa, xb in ((-BOLT_X, 0.0), (0.0, BOLT_X)):
        slots.append(arc_slot(xa, xb, sz * BOLT_Z, lo, hi, SLOT_DEPTH, along_x=True))
for sx in (-1, 1):                       # long narrow slots at the sides
    lo, hi = sorted((sx * SIDE_X_IN, sx * SIDE_X_OUT))
    slots.append(arc_slot(-BOLT_Z, BOLT_Z, sx * BOLT_X, lo, hi, SIDE_DEPTH, along_x=False))

for s in slots:
    body = body.cut(s)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
